import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_TIP = 40.0        # centre to lobe tip
LOBE_R = 19.0       # radius of each lobe arc
NOTCH_DEPTH = 29.7  # centre to deepest point of the concave notch
THICK = 20.0        # thickness along X (axis of the nut)
BACK_FILLET = 5.5   # round on the back (-X) outer edge

THREAD_MAJOR_R = 24.0   # M48 internal thread, root radius
THREAD_PITCH = 6.0      # coarse pitch

# ---------------- derived outline geometry ----------------
d = R_TIP - LOBE_R                       # lobe centre distance
num = LOBE_R**2 - NOTCH_DEPTH**2 + math.sqrt(2) * d * NOTCH_DEPTH - d**2
den = 2 * NOTCH_DEPTH - math.sqrt(2) * d - 2 * LOBE_R
NOTCH_R = num / den                      # notch radius tangent to both lobes
e = NOTCH_DEPTH + NOTCH_R                # notch centre distance (on diagonals)


def rot(p, a):
    c, s = math.cos(a), math.sin(a)
    return (p[0] * c - p[1] * s, p[0] * s + p[1] * c)


def outline_points():
    """Return list of (start, mid, end) for 8 tangent arcs, CCW."""
    arcs = []
    # reference quadrant: lobe on +x axis, notch at +45 deg
    cl = (d, 0.0)
    cn = (e / math.sqrt(2), e / math.sqrt(2))
    vx, vy = cn[0] - cl[0], cn[1] - cl[1]
    L = math.hypot(vx, vy)
    t_up = (cl[0] + LOBE_R * vx / L, cl[1] + LOBE_R * vy / L)   # lobe -> notch at +45
    t_dn = (t_up[0], -t_up[1])                                   # lobe -> notch at -45
    tip = (R_TIP, 0.0)
    notch_mid = (NOTCH_DEPTH / math.sqrt(2), NOTCH_DEPTH / math.sqrt(2))
    for k in range(4):
        a = k * math.pi / 2
        # lobe arc from t_dn to t_up through tip
        arcs.append((rot(t_dn, a), rot(tip, a), rot(t_up, a)))
        # notch arc from t_up to next lobe's t_dn through notch bottom
        nxt = rot(t_dn, a + math.pi / 2)
        arcs.append((rot(t_up, a), rot(notch_mid, a), nxt))
    return arcs


arcs = outline_points()
wp = cq.Workplane("YZ").workplane(offset=-THICK / 2).moveTo(*arcs[0][0])
for s, m, en in arcs:
    wp = wp.threePointArc(m, en)
body = wp.close().extrude(THICK)

# round the back (-X) outer edges
body = body.faces("<X").edges().fillet(BACK_FILLET)

# ---------------- threaded bore (ISO profile as annular grooves) ----------------
P = THREAD_PITCH
H = math.sqrt(3) / 2 * P
THREAD_MINOR_R = THREAD_MAJOR_R - 5.0 / 8.0 * H
flank = (THREAD_MAJOR_R - THREAD_MINOR_R) * math.tan(math.radians(30))
root_w = P / 8.0
crest_w = P / 4.0

# one period of the profile as (depth offset, radius), starting at root-flat centre
period = [
    (0.0, THREAD_MAJOR_R),
    (root_w / 2, THREAD_MAJOR_R),
    (root_w / 2 + flank, THREAD_MINOR_R),
    (root_w / 2 + flank + crest_w, THREAD_MINOR_R),
    (root_w / 2 + 2 * flank + crest_w, THREAD_MAJOR_R),
]
# phase: groove roots laid out symmetrically about the mid-plane of the nut
THREAD_PHASE = (THICK / 2 - P / 2) % P
xf = THICK / 2            # +X face
ext = 1.0
prof = []                 # (depth u from +X face, radius)
u0 = THREAD_PHASE - P * math.ceil((THREAD_PHASE + ext) / P)
k = 0
while True:
    base = u0 + k * P
    if base > THICK + ext:
        break
    for du, r in period:
        prof.append((base + du, r))
    k += 1
# clip the profile to [-ext, THICK+ext] with linear interpolation
def r_at(u):
    for (ua, ra), (ub, rb) in zip(prof, prof[1:]):
        if ua <= u <= ub:
            if ub - ua < 1e-9:
                return rb
            return ra + (rb - ra) * (u - ua) / (ub - ua)
    return prof[-1][1]
inner = [(-ext, r_at(-ext))] + [(u, r) for u, r in prof if -ext < u < THICK + ext] + [(THICK + ext, r_at(THICK + ext))]
# remove consecutive duplicates
clean = []
for p in inner:
    if not clean or abs(p[0] - clean[-1][0]) > 1e-6 or abs(p[1] - clean[-1][1]) > 1e-6:
        clean.append(p)
# drop interior points that lie on a straight run (same radius on both sides)
merged = [clean[0]]
for i in range(1, len(clean) - 1):
    if abs(clean[i - 1][1] - clean[i][1]) < 1e-9 and abs(clean[i + 1][1] - clean[i][1]) < 1e-9:
        continue
    merged.append(clean[i])
merged.append(clean[-1])
pts = [(xf + ext, 0.0)] + [(xf - u, r) for u, r in merged] + [(xf - THICK - ext, 0.0)]

cutter = cq.Workplane("XY").polyline(pts).close().revolve(360, (0, 0, 0), (1, 0, 0))
result = body.cut(cutter)

VIEW = {"azimuth": 45, "elevation": 26}
